import cadquery as cq

# Flanged bushing / spacer: plain tube with a central flange that has
# 45-degree chamfers on both faces, plain through bore along Z.

# Driving dimensions (mm)
body_d = 50.0        # outer diameter of the tube body
bore_d = 33.6        # through-bore diameter
flange_d = 61.6      # outer diameter of the central flange
end_len = 12.1       # length of each plain cylindrical end
chamfer_h = 5.6      # axial height of each flange chamfer
flange_w = 6.4       # axial width of the flange's cylindrical land

# cosmetic: where the periodic-surface seams sit (degrees about Z)
outer_seam_angle = 180.0
bore_seam_angle = 45.0

R = body_d / 2.0
r = bore_d / 2.0
Rf = flange_d / 2.0
H = 2 * end_len + 2 * chamfer_h + flange_w

# z levels (part centred on the origin)
z0 = -H / 2.0
z1 = z0 + end_len
z2 = z1 + chamfer_h
z3 = z2 + flange_w
z4 = z3 + chamfer_h
z5 = H / 2.0

# outer half cross-section in the XZ plane (x = radius, z = height)
profile = [
    (0.0, z0),
    (R, z0),
    (R, z1),
    (Rf, z2),
    (Rf, z3),
    (R, z4),
    (R, z5),
    (0.0, z5),
]

outer = (
    cq.Workplane("XZ")
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), outer_seam_angle)
)

# through bore
bore = (
    cq.Workplane("XY")
    .workplane(offset=z0 - 1.0)
    .circle(r)
    .extrude(H + 2.0)
    .rotate((0, 0, 0), (0, 0, 1), bore_seam_angle)
)

result = outer.cut(bore)

VIEW = {"azimuth": 45, "elevation": 26}
